import math
import cadquery as cq

# ======================= driving dimensions (mm) =======================
# main housing tube (axis along Y, front face at -Y, open at the back)
R = 100.0            # tube outer radius
L = 234.0            # tube length
Y0 = -L / 2          # front face plane
Y1 = L / 2           # back face plane
T_FRONT = 18.0       # front end wall thickness
R_IN = 94.0          # tube bore radius
EDGE_CH = 1.0        # small chamfer on the outer rims

# back end: internal conical ring (45 deg funnel) with notches and holes
R_FUNNEL_BACK = 96.0  # funnel radius at the back face
R_FUNNEL_IN = 70.0    # smallest radius (front face of the ring)
FUNNEL_DEPTH = 27.0   # axial depth of the funnel
N_NOTCH = 12
NOTCH_W = 13.0
NOTCH_R = 97.5        # notches reach out to this radius
NOTCH_DEPTH = 16.0    # axial depth of the notches from the back face
D_RING_HOLE = 4.0

# base (vertical axis Z under the tube)
RB = 90.0            # band / neck radius
Z_BAND_BOT = -140.0
R_STEP2 = 83.0
Z_STEP2_BOT = -156.0
R_STEP3 = 76.5
Z_BOTTOM = -171.5

NECK_FLAT = 70.0     # flats on the neck at x = +-NECK_FLAT
Z_RAMP = -110.0      # ramp start on the band at the X sides
RAMP_ANG = 30.0      # ramp angle from horizontal
RAMP_FILLET = 8.0
FLAT_FILLET = 7.0    # between the flats and the tube
NECK_CHAMFER = 16.0  # 45 deg web between neck and tube underside

R_BASE_BORE = 55.0
BASE_FLOOR = 26.0

N_RADIAL = 16        # radial holes around the band
Z_RADIAL = -125.0
D_RADIAL = 8.5
D_RADIAL_CB = 16.0
RADIAL_CB_DEPTH = 7.0

# front face pattern
PHI0 = 4.0           # angular offset of the front pattern (deg)
N_BOLT = 12
R_BOLT = 92.5
D_BOLT = 5.0
D_BOLT_CB = 10.5
BOLT_CB_DEPTH = 6.0
BOLT_DEPTH = 16.0

R_BORE = 36.0
R_CB1 = 41.0
CB1_DEPTH = 7.0
R_CB2 = 46.0
CB2_DEPTH = 5.0

WIN_IN = 50.0        # window inner straight edge (distance from axis)
WIN_OUT = 83.0       # window outer arc radius (shallow outer pocket)
WIN_STEP_DEPTH = 8.0 # depth of that outer pocket
WIN_OUT_THRU = 70.0  # outer arc radius of the through opening
WIN_HALF = 42.0      # window half length
WIN_FILLET = 6.0
HUB_SHORT = 59.7     # short sides of the recessed hub octagon
HUB_DEPTH = 3.0

R_PIN = 83.5         # pin holes on the window rims
D_PIN = 3.5
R_HUB_S = 50.0       # small holes on the hub
D_HUB_S = 3.0
R_HUB_L = 54.2
D_HUB_L = 4.5

# bottom face pattern
N_POCKET = 6
POCKET_ROT = 7.0
POCKET_R_IN = 47.0
POCKET_R_OUT = 67.0
POCKET_HALF_ANG = 24.0
POCKET_DEPTH = 6.0
POCKET_FILLET = 4.0
R_BOT_STEP = 40.0
BOT_STEP_DEPTH = 1.5
N_BOT_HOLES = 18
R_BOT_HOLES = 33.0
D_BOT_HOLES = 4.5
R_BOT_CENTER = 18.0
BOT_CENTER_DEPTH = 4.0

SEAM_ANG = 90.0      # where the unavoidable cylinder seams are put (least visible)

VIEW = {"azimuth": 45, "elevation": 26}


def pol(r, a_deg):
    a = math.radians(a_deg)
    return (r * math.cos(a), r * math.sin(a))


def front_wp(offset=0.0):
    """Workplane on the front face: local x = +X, local y = +Z, normal -Y.
    Negative extrusion goes into the part (+Y)."""
    return cq.Workplane("XZ", origin=(0, Y0 + offset, 0))


def y_cyl(r, y_start, length):
    """Cylinder along +Y starting at y_start, seam turned to the bottom."""
    return (cq.Workplane("XZ", origin=(0, y_start + length, 0)).circle(r)
            .extrude(length).rotate((0, 0, 0), (0, 1, 0), 90))


def z_cyl(r, z_start, length):
    """Cylinder along +Z, seam turned to SEAM_ANG."""
    return (cq.Workplane("XY", origin=(0, 0, z_start)).circle(r)
            .extrude(length).rotate((0, 0, 0), (0, 0, 1), SEAM_ANG))


# ======================= main tube =======================
tube = y_cyl(R, Y0, L)

# ======================= neck, web and side flats =======================
neck = z_cyl(RB, Z_BAND_BOT, -Z_BAND_BOT)
body = tube.union(neck)
# 45 deg web all around the junction of the neck with the tube underside
body = body.edges(
    cq.selectors.BoxSelector((-RB - 5, -RB - 5, -R - 5), (RB + 5, RB + 5, -30))
).edges("%BSPLINE").chamfer(NECK_CHAMFER)

# flats with a 30 deg ramp on the +-X sides (the tube itself is not touched)
t_r = math.tan(math.radians(RAMP_ANG))
z_flat_bot = Z_RAMP + (RB - NECK_FLAT) * t_r
flat_prof = [
    (NECK_FLAT, 60.0),
    (NECK_FLAT, z_flat_bot),
    (RB, Z_RAMP),
    (RB + 40, Z_RAMP - 40 * t_r),
    (RB + 40, 60.0),
]
flat_cut = None
for s_ in (1, -1):
    pts = [(s_ * x, z) for (x, z) in flat_prof]
    c = (cq.Workplane("XZ", origin=(0, Y1 + 10, 0))
         .polyline(pts).close().extrude(L + 20))
    flat_cut = c if flat_cut is None else flat_cut.union(c)
flat_cut = flat_cut.cut(tube)
body = body.cut(flat_cut)
try:
    body = body.edges(
        cq.selectors.BoxSelector((-NECK_FLAT - 1, -RB, z_flat_bot - 1),
                                 (NECK_FLAT + 1, RB, z_flat_bot + 1))
    ).edges("|Y").fillet(RAMP_FILLET)
except Exception:
    pass

z_flat_top = -math.sqrt(R ** 2 - NECK_FLAT ** 2)
try:
    body = body.edges(
        cq.selectors.BoxSelector((-NECK_FLAT - 1, -R, z_flat_top - 1),
                                 (NECK_FLAT + 1, R, z_flat_top + 1))
    ).edges("|Y").fillet(FLAT_FILLET)
except Exception:
    pass

# ======================= stepped base =======================
body = (body.union(z_cyl(R_STEP2, Z_STEP2_BOT, Z_BAND_BOT - Z_STEP2_BOT))
        .union(z_cyl(R_STEP3, Z_BOTTOM, Z_STEP2_BOT - Z_BOTTOM)))

# rim chamfers
body = body.faces("<Y").edges("%CIRCLE").chamfer(EDGE_CH)
body = body.faces("<Z").edges("%CIRCLE").chamfer(EDGE_CH)
body = body.faces(">Y").edges("%CIRCLE").chamfer(EDGE_CH)

# ======================= hollowing =======================
body = body.cut(y_cyl(R_IN, Y0 + T_FRONT, L - T_FRONT + 1))
body = body.cut(z_cyl(R_BASE_BORE, Z_BOTTOM + BASE_FLOOR,
                      -Z_BOTTOM - BASE_FLOOR - 60))

# conical ring inside the back end (bore ring minus a 45 deg cone, seam turned down)
funnel = cq.Workplane("XY").add(cq.Solid.makeCone(
    R_FUNNEL_IN, R_FUNNEL_BACK, FUNNEL_DEPTH,
    pnt=cq.Vector(0, Y1 - FUNNEL_DEPTH, 0), dir=cq.Vector(0, 1, 0))
).rotate((0, 0, 0), (0, 1, 0), 180)
ring = y_cyl(R_IN + 1.0, Y1 - FUNNEL_DEPTH, FUNNEL_DEPTH).cut(funnel)
body = body.union(ring)
notches = None
rholes = None
for k in range(N_NOTCH):
    a = 30.0 * k
    # U-shaped slot (round end inside), cut radially through the funnel
    nb = (cq.Workplane("YZ", origin=(R_FUNNEL_IN - 8, 0, 0))
          .center(Y1, 0)
          .slot2D(2 * NOTCH_DEPTH, NOTCH_W, 0)
          .extrude(NOTCH_R - R_FUNNEL_IN + 8)
          .rotate((0, 0, 0), (0, 1, 0), -a))
    hb = (cq.Workplane("YZ", origin=(R_FUNNEL_IN - 5, 0, 0))
          .circle(D_RING_HOLE / 2).extrude(NOTCH_R - R_FUNNEL_IN + 5)
          .translate((0, Y1 - FUNNEL_DEPTH * 0.55, 0))
          .rotate((0, 0, 0), (0, 1, 0), -(a + 15.0)))
    notches = nb if notches is None else notches.union(nb)
    rholes = hb if rholes is None else rholes.union(hb)
body = body.cut(notches).cut(rholes)

# ======================= radial holes in the band =======================
rad_cut = None
for k in range(N_RADIAL):
    a = k * 360.0 / N_RADIAL
    h = (cq.Workplane("YZ", origin=(R_BASE_BORE - 5, 0, Z_RADIAL))
         .circle(D_RADIAL / 2).extrude(RB - R_BASE_BORE + 15))
    cb = (cq.Workplane("YZ", origin=(RB - RADIAL_CB_DEPTH, 0, Z_RADIAL))
          .circle(D_RADIAL_CB / 2).extrude(RADIAL_CB_DEPTH + 10))
    hc = h.union(cb).rotate((0, 0, 0), (0, 0, 1), a)
    rad_cut = hc if rad_cut is None else rad_cut.union(hc)
body = body.cut(rad_cut)

# ======================= front face =======================
# recessed hub (octagon): long sides are the window inner edges
lines = []
for k in range(4):
    lines.append((PHI0 + 30 + 90 * k, WIN_IN))
    lines.append((PHI0 + 75 + 90 * k, HUB_SHORT))


def line_isect(l1, l2):
    a1, d1 = math.radians(l1[0]), l1[1]
    a2, d2 = math.radians(l2[0]), l2[1]
    det = math.cos(a1) * math.sin(a2) - math.sin(a1) * math.cos(a2)
    x = (d1 * math.sin(a2) - d2 * math.sin(a1)) / det
    y = (math.cos(a1) * d2 - math.cos(a2) * d1) / det
    return (x, y)


hub_pts = [line_isect(lines[i], lines[(i + 1) % 8]) for i in range(8)]
body = body.cut(front_wp(-1).polyline(hub_pts).close().extrude(-(HUB_DEPTH + 1)))

# bore with counterbores
body = body.cut(front_wp(-1).circle(R_BORE).extrude(-(T_FRONT + 2)))
body = body.cut(front_wp(-1).circle(R_CB1).extrude(-(HUB_DEPTH + CB1_DEPTH + 1)))
body = body.cut(front_wp(-1).circle(R_CB2).extrude(-(HUB_DEPTH + CB2_DEPTH + 1)))

# four windows: stepped (outer pocket, then a smaller through opening)
def window_tool(r_out, depth, half, fil):
    u_end = math.sqrt(r_out ** 2 - half ** 2)
    tool = None
    for k in range(4):
        a = PHI0 + 30 + 90 * k
        w = (cq.Workplane("XZ", origin=(0, Y0 - 1, 0))
             .moveTo(WIN_IN, -half)
             .lineTo(u_end, -half)
             .threePointArc((r_out, 0), (u_end, half))
             .lineTo(WIN_IN, half)
             .close()
             .extrude(-(depth + 1)))
        w = w.edges("|Y").fillet(fil)
        w = w.rotate((0, 0, 0), (0, 1, 0), -a)
        tool = w if tool is None else tool.union(w)
    return tool


body = body.cut(window_tool(WIN_OUT, WIN_STEP_DEPTH, WIN_HALF, WIN_FILLET))
body = body.cut(window_tool(WIN_OUT_THRU, T_FRONT + 1, WIN_HALF - 2.0, 3.0))

# bolt holes
bolt_pts = [pol(R_BOLT, PHI0 + 30 * k) for k in range(N_BOLT)]
body = body.cut(front_wp(-1).pushPoints(bolt_pts).circle(D_BOLT_CB / 2)
                .extrude(-(BOLT_CB_DEPTH + 1)))
body = body.cut(front_wp(-1).pushPoints(bolt_pts).circle(D_BOLT / 2)
                .extrude(-(BOLT_DEPTH + 1)))

# pin holes on the window rims
pin_pts = [pol(R_PIN, 30 * k) for k in range(12) if k % 3 != 0]
body = body.cut(front_wp(-1).pushPoints(pin_pts).circle(D_PIN / 2)
                .extrude(-(T_FRONT + 2)))

# small holes on the hub
hs_pts = []
for k in range(4):
    c = PHI0 + 30 + 90 * k
    hs_pts += [pol(R_HUB_S, c - 22.5), pol(R_HUB_S, c + 22.5)]
hl_pts = [pol(R_HUB_L, PHI0 + 75 + 90 * k) for k in range(4)]
body = body.cut(front_wp(-1).pushPoints(hs_pts).circle(D_HUB_S / 2)
                .extrude(-(HUB_DEPTH + 8)))
body = body.cut(front_wp(-1).pushPoints(hl_pts).circle(D_HUB_L / 2)
                .extrude(-(HUB_DEPTH + 8)))

# ======================= bottom face =======================
pk_cut = None
for k in range(N_POCKET):
    a = POCKET_ROT + k * 360.0 / N_POCKET
    a0, a1 = a - POCKET_HALF_ANG, a + POCKET_HALF_ANG
    p = (cq.Workplane("XY", origin=(0, 0, Z_BOTTOM - 1))
         .moveTo(*pol(POCKET_R_IN, a0))
         .lineTo(*pol(POCKET_R_OUT, a0))
         .threePointArc(pol(POCKET_R_OUT, a), pol(POCKET_R_OUT, a1))
         .lineTo(*pol(POCKET_R_IN, a1))
         .threePointArc(pol(POCKET_R_IN, a), pol(POCKET_R_IN, a0))
         .close()
         .extrude(POCKET_DEPTH + 1))
    p = p.edges("|Z").fillet(POCKET_FILLET)
    pk_cut = p if pk_cut is None else pk_cut.union(p)
body = body.cut(pk_cut)
pk_holes = [pol((POCKET_R_IN + POCKET_R_OUT) / 2, POCKET_ROT + k * 360.0 / N_POCKET)
            for k in range(N_POCKET)]
body = body.cut(cq.Workplane("XY", origin=(0, 0, Z_BOTTOM - 1))
                .pushPoints(pk_holes).circle(2.0).extrude(POCKET_DEPTH + 9))

body = body.cut(cq.Workplane("XY", origin=(0, 0, Z_BOTTOM - 1))
                .circle(R_BOT_STEP).extrude(BOT_STEP_DEPTH + 1))
body = body.cut(cq.Workplane("XY", origin=(0, 0, Z_BOTTOM - 1))
                .circle(R_BOT_CENTER).extrude(BOT_CENTER_DEPTH + 1))
bh_pts = [pol(R_BOT_HOLES, k * 360.0 / N_BOT_HOLES) for k in range(N_BOT_HOLES)]
body = body.cut(cq.Workplane("XY", origin=(0, 0, Z_BOTTOM - 1))
                .pushPoints(bh_pts).circle(D_BOT_HOLES / 2).extrude(11))
body = body.cut(cq.Workplane("XY", origin=(0, 0, Z_BOTTOM - 1))
                .circle(2.0).extrude(14))

result = body
